import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet

# ---- driving dimensions (mm) ----
L = 160.0          # overall length along X
W = 51.2           # overall width along Y (without the tabs)
H = 29.8           # overall height along Z
T_FLOOR = 2.0      # floor thickness

T_SIDE = 3.7       # thickness of the two long walls (-Y / +Y)
R_SIDE_OUT = 2.2   # long-wall rim: outer rounding
R_SIDE_IN = 1.45   # long-wall rim: inner rounding

T_XP = 3.0         # thickness of the +X end wall
R_XP_OUT = 1.0     # +X end rim: outer rounding
R_XP_IN = 1.95     # +X end rim: inner rounding

T_XN = 2.85        # thickness of the -X end wall
R_XN_IN = 2.75     # -X end rim: inner quarter-round (outer edge stays sharp)

TAB_W = 20.5       # mounting tab width along X (flush with the X ends)
TAB_D = 4.6        # tab projection beyond the +Y wall
TAB_H = 4.5        # tab height
TAB_R = 0.8        # rounding of the tab's free top edges

EPS = 1e-3

# inner pocket extents
X_IN0 = -L / 2 + T_XN
X_IN1 = L / 2 - T_XP
Y_IN = W / 2 - T_SIDE


def near(a, b):
    return abs(a - b) < EPS


def top_edge(shape, axis, value):
    """The straight edge lying in the top plane z = H at x = value (axis 'x') or y = value (axis 'y')."""
    for e in shape.Edges():
        bb = e.BoundingBox()
        if not (near(bb.zmin, H) and near(bb.zmax, H)):
            continue
        if axis == "x" and near(bb.xmin, value) and near(bb.xmax, value):
            return e
        if axis == "y" and near(bb.ymin, value) and near(bb.ymax, value):
            return e
    raise ValueError(f"no top edge at {axis}={value}")


def fillet_variable(shape, edge_radii):
    mk = BRepFilletAPI_MakeFillet(shape.wrapped)
    for e, r in edge_radii:
        mk.Add(r, e.wrapped)
    mk.Build()
    return cq.Solid(mk.Shape())


# ---- open tray: block minus pocket ----
block = cq.Workplane("XY").box(L, W, H, centered=(True, True, False))
pocket = (
    cq.Workplane("XY", origin=((X_IN0 + X_IN1) / 2, 0, T_FLOOR))
    .rect(X_IN1 - X_IN0, 2 * Y_IN)
    .extrude(H)
)
tray = block.cut(pocket).val()

# rounded rim, outer edges (the -X end keeps a sharp outer top edge)
tray = fillet_variable(tray, [
    (top_edge(tray, "y", -W / 2), R_SIDE_OUT),
    (top_edge(tray, "y", W / 2), R_SIDE_OUT),
    (top_edge(tray, "x", L / 2), R_XP_OUT),
])
# rounded rim, inner edges
tray = fillet_variable(tray, [
    (top_edge(tray, "y", -Y_IN), R_SIDE_IN),
    (top_edge(tray, "y", Y_IN), R_SIDE_IN),
    (top_edge(tray, "x", X_IN1), R_XP_IN),
    (top_edge(tray, "x", X_IN0), R_XN_IN),
])
tray = cq.Workplane("XY").add(tray)

# ---- mounting tabs on the +Y side, flush with the X ends ----
OVERLAP = 0.5
for sx in (-1, 1):
    cx = sx * (L / 2 - TAB_W / 2)
    tab = (
        cq.Workplane("XY")
        .box(TAB_W, TAB_D + OVERLAP, TAB_H, centered=(True, False, False))
        .translate((cx, W / 2 - OVERLAP, 0))
        .faces(">Z").edges("not <Y")
        .fillet(TAB_R)
    )
    tray = tray.union(tab)

result = tray

VIEW = {"azimuth": 45, "elevation": 26}
